import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
MODULE = 2.0            # gear module
N_TEETH = 11            # number of teeth
PRESSURE_ANGLE = 22.8   # deg (transverse)
HELIX_ANGLE = 30.0      # deg, herringbone helix angle (at pitch circle)
GEAR_W = 10.0           # face width of the herringbone gear
HUB_D = 16.65           # hub outer diameter (just inside the root circle)
HUB_H = 18.0            # hub height above the gear face
BORE_D = 8.8            # through bore
PHASE = -1.1            # deg, angular position of a tooth on the bottom face
TOOTH_THIN = 0.6        # deg, backlash: angular thinning of each tooth
FLANK_PTS = 7           # interpolation points per involute flank

VIEW = {"azimuth": 45, "elevation": 26}

# derived gear geometry
R_PITCH = MODULE * N_TEETH / 2.0
R_TIP = R_PITCH + MODULE
R_ROOT = R_PITCH - 1.25 * MODULE
R_BASE = R_PITCH * math.cos(math.radians(PRESSURE_ANGLE))
# twist of each half of the herringbone (rotation between face and mid plane)
HALF_TWIST = math.degrees((GEAR_W / 2.0) * math.tan(math.radians(HELIX_ANGLE)) / R_PITCH)


def _inv(a):
    return math.tan(a) - a


def _rot(p, a):
    c, s = math.cos(a), math.sin(a)
    return (p[0] * c - p[1] * s, p[0] * s + p[1] * c)


def _v(p):
    return cq.Vector(p[0], p[1], 0.0)


def _polar(r, a):
    return (r * math.cos(a), r * math.sin(a))


def _ang(p):
    return math.atan2(p[1], p[0])


def _arc(p0, p1, r):
    a0 = _ang(p0)
    a1 = _ang(p1)
    while a1 < a0:
        a1 += 2 * math.pi
    return cq.Edge.makeThreePointArc(_v(p0), _v(_polar(r, 0.5 * (a0 + a1))), _v(p1))


def gear_outline():
    """Closed wire of an involute gear outline (one tooth centred on +X):
    root arc - radial line - involute flank - tip arc - involute flank - radial line."""
    z = N_TEETH
    alpha = math.radians(PRESSURE_ANGLE)
    rb = R_BASE
    # half tooth angle at base circle (less half the backlash allowance)
    half_base = math.pi / (2 * z) + _inv(alpha) - math.radians(TOOTH_THIN) / 2.0
    t_max = math.sqrt((R_TIP / rb) ** 2 - 1.0)
    pitch = 2 * math.pi / z

    def inv_pt(t):
        return (rb * (math.cos(t) + t * math.sin(t)),
                rb * (math.sin(t) - t * math.cos(t)))

    ts = [t_max * k / (FLANK_PTS - 1) for k in range(FLANK_PTS)]
    edges = []
    first_start = None
    prev_end = None
    for i in range(z):
        ca = i * pitch
        # one smooth flank: radial run-in from the root circle, then involute
        r_in = _polar(R_ROOT, ca - half_base)
        l_in = _polar(R_ROOT, ca + half_base)
        r_mid = _polar(0.5 * (R_ROOT + rb), ca - half_base)
        l_mid = _polar(0.5 * (R_ROOT + rb), ca + half_base)
        right = [r_in, r_mid] + [_rot(inv_pt(t), ca - half_base) for t in ts]
        left = [_rot((inv_pt(t)[0], -inv_pt(t)[1]), ca + half_base) for t in reversed(ts)] + [l_mid, l_in]
        if prev_end is None:
            first_start = r_in
        else:
            edges.append(_arc(prev_end, r_in, R_ROOT))
        edges.append(cq.Edge.makeSpline([_v(p) for p in right]))
        edges.append(_arc(right[-1], left[0], R_TIP))
        edges.append(cq.Edge.makeSpline([_v(p) for p in left]))
        prev_end = l_in
    edges.append(_arc(prev_end, first_start, R_ROOT))
    w = cq.Wire.assembleEdges(edges)
    return w.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), PHASE)


gear_wire = gear_outline()
half = GEAR_W / 2.0

# Herringbone: lower half twists clockwise (seen from above) up to the mid
# plane, upper half twists back counter-clockwise to the top face.
bottom_half = (
    cq.Workplane("XY")
    .add(gear_wire)
    .toPending()
    .twistExtrude(half, -HALF_TWIST)
)
mid_wire = gear_wire.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), -HALF_TWIST).translate(
    cq.Vector(0, 0, half))
top_half = (
    cq.Workplane("XY", origin=(0, 0, half))
    .add(mid_wire)
    .toPending()
    .twistExtrude(half, HALF_TWIST)
)
gear = bottom_half.union(top_half)

# hub boss on top of the gear (cylinder seam turned towards +Y)
HUB_SEAM = 90.0         # deg
BORE_SEAM = 225.0       # deg
hub = cq.Workplane("XY").add(
    cq.Solid.makeCylinder(HUB_D / 2.0, HUB_H + 0.5,
                          cq.Vector(0, 0, GEAR_W - 0.5), cq.Vector(0, 0, 1))
    .rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), HUB_SEAM)
)
body = gear.union(hub)

# through bore
bore = cq.Workplane("XY").add(
    cq.Solid.makeCylinder(BORE_D / 2.0, GEAR_W + HUB_H + 2.0,
                          cq.Vector(0, 0, -1.0), cq.Vector(0, 0, 1))
    .rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), BORE_SEAM)
)
result = body.cut(bore)
